import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 54.5          # overall length along X (flange -X end to +X end)
W = 50.1          # flange width along Y
WB = 37.8         # body (cover) width along Y
H = 30.0          # overall height
R = 6.0           # radius of the cover's rounded top edges
XB0 = 1.2         # X where the cover body starts
ZF = 8.0          # flange top height
ZE = 5.64         # underside of the flange ears at the -X end
XL = 14.3         # X where the solid lower flange block starts
XT = 13.3         # X where the -X end block (tunnel) ends and the cavity starts
YI = 14.95        # inner half-width of the lower flange blocks and cavity
T_END = 2.3       # +X end wall thickness
CAV_Z = 25.25     # cavity ceiling height
# -X end cable tunnel (mouse hole)
TUN_HW = YI       # tunnel half width (flush with the cavity walls)
TUN_H = 16.1      # tunnel height
TUN_R = 3.0       # tunnel top corner radius
# ears / feet at -X end
FOOT_YC = 19.9    # |Y| centre of the upper foot pads
FOOT1_W = 5.8     # upper foot layer width
FOOT1_X0 = 0.2
FOOT1_Z0 = 3.13
FOOT1_R = 2.6     # corner radius of the upper pad's -X end
FOOT2_W = 3.4     # lower foot layer width
FOOT2_YC = 19.55  # |Y| centre of the lower foot pads
FOOT2_X0 = 0.87
FOOT2_X1 = 11.8
FOOT2_R = 1.1     # corner radius of the lower pad
# holes
HOLE_D = 3.8
HOLE_X = (16.45, 49.0)
HOLE_Y = 22.4
TOP_HOLE_D = 3.8
TOP_HOLE_X = 38.7
# top U slots (spring tongues)
SL_X0, SL_X1 = 22.0, 43.1
SL_YI, SL_YO = 3.05, 11.05
SL_W = 1.2
# +X end window
WIN_W, WIN_Z0, WIN_Z1 = 15.8, 19.3, 25.6
# detent pins under the free ends of the spring tongues
PIN_D, PIN_YC, PIN_Z0, PIN_XOFF = 3.3, 7.05, 23.1, 0.3
# back notch / window
NT_X0, NT_X1 = 25.3, 40.4
NT_YO = 22.66
NT_Z1 = 12.8


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def arch_solid(x0, x1, hw, z0, ztop, r):
    """Prism along X whose YZ profile is a rectangle |y|<=hw, z0..ztop with
    both top corners rounded (radius r)."""
    prism = (cq.Workplane("YZ").workplane(offset=x0)
             .center(0, (z0 + ztop) / 2).rect(2 * hw, ztop - z0)
             .extrude(x1 - x0))
    return prism.edges("|X and >Z").fillet(r)


# ---- cover body (arched profile extruded along X) ----
body = arch_solid(XB0, L, WB / 2, 0, H, R)

# ---- lower flange block (front/back flanges + lower walls) ----
body = body.union(box(XL, L, -W / 2, W / 2, 0, ZF))

# ---- ears at the -X end ----
for s in (1, -1):
    y0, y1 = sorted((s * TUN_HW, s * W / 2))
    body = body.union(box(0, XL, y0, y1, ZE, ZF))

# ---- main cavity (open to the bottom) ----
cav = box(XT, L - T_END, -YI, YI, -1, CAV_Z)
body = body.cut(cav)

# ---- -X end cable tunnel through the solid end block ----
tun = arch_solid(-1, XT + 0.01, TUN_HW, -1, TUN_H, TUN_R)
body = body.cut(tun)

# ---- clear everything under the ears at the -X end (only the feet remain) ----
body = body.cut(box(-1, XL, -W, W, -1, ZE))

# ---- feet under the ears (two stacked pads) ----
for s in (1, -1):
    yc = s * FOOT_YC
    # upper pad: rounded at its -X end, runs into the lower flange block
    f1 = box(FOOT1_X0, XL + 0.01, yc - FOOT1_W / 2, yc + FOOT1_W / 2, FOOT1_Z0, ZE + 0.01)
    f1 = f1.edges("|Z and <X").fillet(FOOT1_R)
    # lower pad: small rounded rectangle
    y2 = s * FOOT2_YC
    f2 = box(FOOT2_X0, FOOT2_X1, y2 - FOOT2_W / 2, y2 + FOOT2_W / 2, 0, FOOT1_Z0 + 0.01)
    f2 = f2.edges("|Z").fillet(FOOT2_R)
    body = body.union(f1).union(f2)

# ---- flange mounting holes ----
pts = [(x, s * HOLE_Y) for x in HOLE_X for s in (1, -1)]
holes = (cq.Workplane("XY").workplane(offset=-1).pushPoints(pts)
         .circle(HOLE_D / 2).extrude(ZF + 2))
body = body.cut(holes)

# ---- top hole ----
th = (cq.Workplane("XY").workplane(offset=CAV_Z - 1).center(TOP_HOLE_X, 0)
      .circle(TOP_HOLE_D / 2).extrude(H - CAV_Z + 3))
body = body.cut(th)

# ---- U-shaped spring-tongue slots ----
for s in (1, -1):
    yi, yo = s * SL_YI, s * SL_YO
    zs0, zs1 = CAV_Z - 1, H + 1
    legs = [
        (SL_X0, SL_X1, yi, yi + s * SL_W),
        (SL_X0, SL_X1, yo - s * SL_W, yo),
        (SL_X1 - SL_W, SL_X1, yi, yo),
    ]
    for x0, x1, y0, y1 in legs:
        ya, yb = sorted((y0, y1))
        body = body.cut(box(x0, x1, ya, yb, zs0, zs1))

# ---- +X end window ----
body = body.cut(box(L - T_END, L + 1, -WIN_W / 2, WIN_W / 2, WIN_Z0, WIN_Z1))

# ---- detent pins hanging under the free ends of the tongues ----
for s in (1, -1):
    pin_plane = cq.Plane(origin=(SL_X1 - SL_W - PIN_XOFF - PIN_D / 2, s * PIN_YC, PIN_Z0),
                         xDir=(-1, 0, 0), normal=(0, 0, 1))
    pin = (cq.Workplane(pin_plane)
           .circle(PIN_D / 2).extrude(CAV_Z - PIN_Z0 + 0.01))
    pin = pin.faces("<Z").edges().fillet(0.5)
    body = body.union(pin)

# ---- back notch through the flange and lower back wall ----
body = body.cut(box(NT_X0, NT_X1, YI - 1, NT_YO, -1, NT_Z1))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
